import cadquery as cq

# Perforated square plate with a square grid of sharp-cornered square holes
PLATE = 300.0        # plate side length (mm)
THK = 2.5            # plate thickness
N = 16               # holes per row / column
PITCH = 18.47        # hole pitch (centre to centre)
HOLE = 9.5           # square hole side

# plain square plate, centred on the origin, lying in the XY plane
plate = cq.Workplane("XY").box(PLATE, PLATE, THK)

# centred N x N grid of hole centres
pts = [((i - (N - 1) / 2) * PITCH, (j - (N - 1) / 2) * PITCH)
       for i in range(N) for j in range(N)]

# through-cutting square prisms
cutter = (cq.Workplane("XY").workplane(offset=-THK)
          .pushPoints(pts)
          .rect(HOLE, HOLE)
          .extrude(THK * 2))

result = plate.cut(cutter)

VIEW = {"azimuth": 45, "elevation": 26}
